import cadquery as cq

# =====================================================================
# Open-back box holder with a flanged cup in the top and two
# rectangular windows in the front wall.
#   X = width, Y = depth (front is -Y, open back is +Y), Z = height
# =====================================================================

# ---------------- driving dimensions (mm) ----------------
W = 50.9            # box width  (X)
D = 46.3            # box depth  (Y)
H = 60.0            # box height (Z)
T = 2.3             # wall thickness (all walls)
R_EDGE = 2.1        # outer edge fillet radius

CUP_OD = 42.0       # flange (rim) outer diameter, sits on the top face
CUP_BODY_OD = 40.0  # cup outer diameter below the top face
CUP_ID = 37.0       # cup bore diameter
RIM_UP = 1.0        # flange height above the top face
CUP_DEPTH = 22.2    # cup depth below the top face (outside bottom)
CUP_FLOOR = 2.0     # cup bottom thickness

WIN_W = 34.8        # window width
WIN_H = 11.5        # window height
WIN1_TOP = 23.0     # top window: distance of its top edge below the top face
WIN_GAP = 7.0       # web between the two windows
WIN_X_OFF = 0.2     # small sideways offset of the windows (+X)

# ---------------- body: filleted box, hollowed, open at the back (+Y) ----------------
outer = (
    cq.Workplane("XY")
    .box(W, D, H, centered=(True, True, False))
    .edges()
    .fillet(R_EDGE)
)
# cavity: walls of thickness T on the front, sides, top and bottom,
# running straight out through the back face
cavity = (
    cq.Workplane("XY")
    .box(W - 2 * T, D, H - 2 * T, centered=(True, False, False))
    .translate((0, -D / 2.0 + T, T))
)
body = outer.cut(cavity)

# ---------------- two windows through the front wall (-Y) ----------------
win_tops = (WIN1_TOP, WIN1_TOP + WIN_H + WIN_GAP)
for top in win_tops:
    zc = H - top - WIN_H / 2.0
    cutter = (
        cq.Workplane("XZ", origin=(WIN_X_OFF, -D / 2.0 - T, zc))
        .rect(WIN_W, WIN_H)
        .extrude(-3 * T)          # XZ normal is -Y, so negative goes inward (+Y)
    )
    body = body.cut(cutter)

# ---------------- flanged cup hanging from the top ----------------
cup_body = (
    cq.Workplane("XY", origin=(0, 0, H - CUP_DEPTH))
    .circle(CUP_BODY_OD / 2.0)
    .extrude(CUP_DEPTH)
)
flange = (
    cq.Workplane("XY", origin=(0, 0, H))
    .circle(CUP_OD / 2.0)
    .extrude(RIM_UP)
)
body = body.union(cup_body).union(flange)

bore = (
    cq.Workplane("XY", origin=(0, 0, H - CUP_DEPTH + CUP_FLOOR))
    .circle(CUP_ID / 2.0)
    .extrude(CUP_DEPTH + RIM_UP)
)
body = body.cut(bore)

result = body

VIEW = {"azimuth": 45, "elevation": 26}
